import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
D = 100.0                 # outer diameter of the disc
R = D / 2.0
T = 13.6                  # overall thickness
FLOOR_Z = 10.4            # underside of the top plate (cavity depth from bottom)
OUTER_BOTTOM_FILLET = 1.6

# internal ring gear on the underside
N_TEETH = 57
MODULE = 1.565
GEAR_PHASE = 1.3          # angular position of the first tooth space (deg)
PRESSURE_ANGLE = 20.0
RP = MODULE * N_TEETH / 2.0          # pitch radius
R_TIP = RP - MODULE                  # internal gear: tips point inwards
R_ROOT = RP + 1.25 * MODULE

# central hub on the underside (revolved profile with rounded edges)
HUB_R = 19.0
HUB_Z0 = 0.0              # hub bottom face height above the rim bottom
HUB_TOP_FILLET = 2.0      # blend hub side -> plate underside
HUB_BOTTOM_ROUND = 3.5    # rounded lower edge of the hub

# radial set-screw bores (M6) through hub and nut traps
BORE_R = 3.3
BOSS_R = 4.0             # round boss around the bore between hub and slot
BORE_TOP_DEPTH = 1.5      # bore top below the top face
BORE_Z = T - BORE_TOP_DEPTH - BORE_R

# top-face cut-outs
HOLE_D = 10.2             # centre through hole (shaft)
TRAP_LEN = 11.4           # nut trap length
TRAP_W = 4.7              # nut trap width
TRAP_OFF = 9.3            # nut trap centre distance from axis
TRAP_CORNER = 0.5
SLOT_R0 = 19.4            # slot inner end radius
SLOT_R1 = 42.1            # slot outer end radius
SLOT_W = 7.6
SLOT_CORNER = 2.2
SLOT_EDGE_FILLET = 1.2    # rounded lower edges of the slots (plate underside)

# directions of the two radial features (degrees about Z): +X and -Y
ARM_ANGLES = [0.0, -90.0]


def rot(shape, ang):
    return shape.rotate((0, 0, 0), (0, 0, 1), ang)


def compound(wps):
    return cq.Compound.makeCompound([w.val() for w in wps])


def through_rrect(cx, length, width, corner):
    """Rounded-rectangle prism through the whole part, centred at (cx, 0)."""
    return (
        cq.Workplane("XY")
        .sketch()
        .push([(cx, 0)])
        .rect(length, width)
        .reset()
        .vertices()
        .fillet(corner)
        .finalize()
        .extrude(T + 2)
        .translate((0, 0, -1))
    )


# ---------------- main disc (seam turned to the back) ----------------
body = cq.Workplane("XY").circle(R).extrude(T).rotate((0, 0, 0), (0, 0, 1), 180)
body = body.faces("<Z").edges().fillet(OUTER_BOTTOM_FILLET)

# ---------------- underside cavity (tip circle of the ring gear) ----------------
body = body.cut(cq.Workplane("XY").circle(R_TIP).extrude(FLOOR_Z))

# ---------------- central hub (revolved, rounded edges) ----------------
rb = HUB_BOTTOM_ROUND
rt = HUB_TOP_FILLET
c45 = math.cos(math.radians(45))
hub = (
    cq.Workplane("XZ")
    .moveTo(0, HUB_Z0)
    .lineTo(HUB_R - rb, HUB_Z0)
    .threePointArc((HUB_R - rb + rb * c45, HUB_Z0 + rb - rb * c45), (HUB_R, HUB_Z0 + rb))
    .lineTo(HUB_R, FLOOR_Z - rt)
    .threePointArc((HUB_R + rt - rt * c45, FLOOR_Z - rt + rt * c45), (HUB_R + rt, FLOOR_Z))
    .lineTo(HUB_R - 2.0, FLOOR_Z)
    .lineTo(HUB_R - 2.0, FLOOR_Z + 1.0)
    .lineTo(0, FLOOR_Z + 1.0)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
body = body.union(hub)

# ---------------- short round bosses carrying the set-screw bores ----------------
for a in ARM_ANGLES:
    boss = cq.Workplane("YZ").center(0, BORE_Z).circle(BOSS_R).extrude(SLOT_R0)
    body = body.union(rot(boss, a))


# ---------------- radial slots with rounded lower edges ----------------
def slot_cutter():
    """Through slot plus the material removed by rounding its lower edge
    along the two long sides and the outer end (the inner end stays square
    where the set-screw bore comes out)."""
    cx = (SLOT_R0 + SLOT_R1) / 2.0
    length = SLOT_R1 - SLOT_R0
    pad = SLOT_EDGE_FILLET + 2.0
    x0 = SLOT_R0 + SLOT_CORNER          # start of the straight long sides
    x1 = SLOT_R1 + pad
    block = (
        cq.Workplane("XY")
        .workplane(offset=FLOOR_Z)
        .center((x0 + x1) / 2.0, 0)
        .rect(x1 - x0, SLOT_W + 2 * pad)
        .extrude(T - FLOOR_Z)
    )
    prism = through_rrect(cx, length, SLOT_W, SLOT_CORNER)
    holed = block.cut(prism)
    m = SLOT_W / 2.0 + 0.5
    edges = sorted(
        holed.edges(
            cq.selectors.BoxSelector((x0 + 0.01, -m, FLOOR_Z - 0.01),
                                     (SLOT_R1 + 0.5, m, FLOOR_Z + 0.01))
        ).vals(),
        key=lambda e: (round(e.Center().x, 3), round(e.Center().y, 3)),
    )
    rounded = holed.newObject([holed.val().fillet(SLOT_EDGE_FILLET, edges)])
    return block.cut(rounded).union(prism)


cutter = slot_cutter()
for a in ARM_ANGLES:
    body = body.cut(rot(cutter, a))

# ---------------- internal gear teeth (tooth spaces, polar pattern) ----------------
pitch = math.pi * MODULE
tpa = math.tan(math.radians(PRESSURE_ANGLE))
space_tip = pitch / 2.0 + 2 * MODULE * tpa          # tooth space width at tip circle
space_root = pitch / 2.0 - 2 * 1.25 * MODULE * tpa  # tooth space width at root circle
space_root = max(space_root, 0.4)
r_in = R_TIP - 0.3
space_in = space_tip + 2 * 0.3 * tpa
tooth_space = (
    cq.Workplane("XY")
    .polyline([
        (r_in, -space_in / 2.0),
        (R_ROOT, -space_root / 2.0),
        (R_ROOT, space_root / 2.0),
        (r_in, space_in / 2.0),
    ])
    .close()
    .extrude(FLOOR_Z)
)
body = body.cut(compound([rot(tooth_space, GEAR_PHASE + 360.0 / N_TEETH * i) for i in range(N_TEETH)]))

# ---------------- centre hole, nut traps and set-screw bores ----------------
hole = cq.Workplane("XY").circle(HOLE_D / 2.0).extrude(T + 2).translate((0, 0, -1))
trap = through_rrect(TRAP_OFF, TRAP_W, TRAP_LEN, TRAP_CORNER)
bore = (
    cq.Workplane("YZ")
    .center(0, BORE_Z)
    .circle(BORE_R)
    .extrude(SLOT_R0 + 1.0)
)
tools = [hole] + [rot(trap, a) for a in ARM_ANGLES] + [rot(bore, a) for a in ARM_ANGLES]
cut_all = tools[0]
for t in tools[1:]:
    cut_all = cut_all.union(t)
body = body.cut(cut_all)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
